import math
import cadquery as cq

# =====================================================================
#  Hex-bodied nozzle / plug: domed cap with an inclined side saw-slot,
#  13 AF hex, M8 threaded shank and a bevel-cut hollow tip.
#  Axis = Z, hex bottom face at z = 0, slot opens toward +X,
#  bevel face of the tip faces +X / down.
# =====================================================================

# ---------------- driving dimensions (mm) ----------------
HEX_AF = 13.0            # hex across flats (flats face +/-X, corners at +/-Y)
HEX_H = 8.0              # hex height (hex bottom at z = 0)

DOME_D = 11.45           # diameter of the domed cap above the hex
DOME_TOTAL_H = 11.45     # cap height above the hex top (straight wall + crown)
CROWN_R_RATIO = 2.0      # crown sphere radius / cap radius
KNUCKLE_R_RATIO = 0.75   # knuckle (torus) radius / cap radius

SLOT_T = 1.35            # saw-slot thickness
SLOT_ANGLE = 17.0        # slot plane tilt, descending toward +X (deg)
SLOT_Z_AXIS = 4.36       # slot mid-plane height on the axis, above hex top
SLOT_END_X = -0.75       # slot end face (square to the slot) reaches past the axis

THREAD_D = 8.1           # thread major diameter
THREAD_MINOR_D = 6.8     # thread minor diameter
THREAD_PITCH = 0.975
THREAD_L = 9.9           # threaded length below the hex
THREAD_CREST_FLAT = 0.08 # small flat on the thread crests

TIP_D = 6.8              # plain tip below the thread
TIP_L = 5.995            # tip length on its long (-X) side
TIP_CUT_ANGLE = 38.3     # bevel of the tip cut from horizontal (deg)

BORE_D = 3.25            # bore from the tip up into the slot

SEAM_ANGLE = 180.0       # park the seams of revolved faces on the back side


def seam_back(wp):
    """Rotate a solid of revolution about Z so its seam sits at the back."""
    return wp.rotate((0, 0, 0), (0, 0, 1), SEAM_ANGLE)


# ---------------- hex ----------------
hex_body = (
    cq.Workplane("XY")
    .polygon(6, HEX_AF / math.cos(math.radians(30)))
    .extrude(HEX_H)
    # polygon() puts a corner on +X; turn 30 deg so corners sit on +/-Y
    .rotate((0, 0, 0), (0, 0, 1), 30)
)

# ---------------- domed cap (straight wall + knuckle + crown) ----------------
R = DOME_D / 2.0
Rc = CROWN_R_RATIO * R                   # crown sphere radius
rk = KNUCKLE_R_RATIO * R                 # knuckle radius
crown_rise = Rc - math.sqrt((Rc - rk) ** 2 - (R - rk) ** 2)
z0 = HEX_H
z_top = z0 + DOME_TOTAL_H
z_k = z_top - crown_rise                 # end of the straight wall
ckx, ckz = R - rk, z_k                   # knuckle centre
ccx, ccz = 0.0, z_top - Rc               # crown centre
dl = math.hypot(ckx - ccx, ckz - ccz)
ux, uz = (ckx - ccx) / dl, (ckz - ccz) / dl
tx, tz = ccx + Rc * ux, ccz + Rc * uz    # tangent point knuckle -> crown
th_t = math.atan2(uz, ux)
k_mid = (ckx + rk * math.cos(th_t / 2), ckz + rk * math.sin(th_t / 2))
th_c = (th_t + math.pi / 2) / 2
c_mid = (ccx + Rc * math.cos(th_c), ccz + Rc * math.sin(th_c))

cap = seam_back(
    cq.Workplane("XZ")
    .moveTo(0, z0 - 0.5)
    .lineTo(R, z0 - 0.5)
    .lineTo(R, z_k)
    .threePointArc(k_mid, (tx, tz))
    .threePointArc(c_mid, (0, z_top))
    .close()
    .revolve(360, (0, 0, 0), (0, 1, 0))
)

body = hex_body.union(cap)

# ---------------- shank core (minor diameter) + tip ----------------
z_low = -(THREAD_L + TIP_L)              # lowest point of the bevelled tip
core = seam_back(
    cq.Workplane("XZ")
    .moveTo(0, z_low - 1.0)
    .lineTo(TIP_D / 2.0, z_low - 1.0)
    .lineTo(TIP_D / 2.0, 0.5)
    .lineTo(0, 0.5)
    .close()
    .revolve(360, (0, 0, 0), (0, 1, 0))
)
body = body.union(core)

# ---------------- thread: V rings at the pitch (plain geometry, no helix) ----------------
r_min = THREAD_MINOR_D / 2.0 - 0.05
r_maj = THREAD_D / 2.0
crest = THREAD_CREST_FLAT / 2.0
tooth = seam_back(
    cq.Workplane("XZ")
    .moveTo(r_min, -THREAD_PITCH / 2.0)
    .lineTo(r_maj, -crest)
    .lineTo(r_maj, crest)
    .lineTo(r_min, THREAD_PITCH / 2.0)
    .close()
    .revolve(360, (0, 0, 0), (0, 1, 0))
)
n_teeth = int(THREAD_L / THREAD_PITCH)  # teeth stacked up from the thread end
teeth = None
for i in range(n_teeth):
    t = tooth.translate((0, 0, -THREAD_L + THREAD_PITCH * (i + 0.5)))
    teeth = t if teeth is None else teeth.union(t)
body = body.union(teeth)

# run-out of the (real, helical) thread: the last half turn sits lower on the
# +X / +Y side, so add a partial tooth ring there (trimmed by the bevel below)
RUNOUT_START = 0.0       # deg, from +X
RUNOUT_SPAN = 150.0      # deg, toward +Y
runout = (
    cq.Workplane("XZ")
    .moveTo(r_min, -THREAD_PITCH / 2.0)
    .lineTo(r_maj, -crest)
    .lineTo(r_maj, crest)
    .lineTo(r_min, THREAD_PITCH / 2.0)
    .close()
    .revolve(RUNOUT_SPAN, (0, 0, 0), (0, 1, 0))
    .rotate((0, 0, 0), (0, 0, 1), RUNOUT_START)
    .translate((0, 0, -THREAD_L))
)
body = body.union(runout)

# ---------------- bevel cut of the tip (face looks toward +X and down) ----------------
bevel_rise = TIP_D * math.tan(math.radians(TIP_CUT_ANGLE))
cutter = (
    cq.Workplane("XY")
    .box(60, 60, 60)
    .translate((0, 0, -30))
    .rotate((0, 0, 0), (0, 1, 0), -TIP_CUT_ANGLE)
    .translate((0, 0, z_low + bevel_rise / 2.0))
)
body = body.cut(cutter)

# ---------------- axial bore, running up into the slot ----------------
z_slot = z0 + SLOT_Z_AXIS
bore = seam_back(
    cq.Workplane("XY")
    .workplane(offset=z_low - 2.0)
    .circle(BORE_D / 2.0)
    .extrude(z_slot - (z_low - 2.0))
)
body = body.cut(bore)

# ---------------- inclined saw slot entering the cap from +X ----------------
u_end = SLOT_END_X / math.cos(math.radians(SLOT_ANGLE))
SLOT_LEN = 20.0
slot = (
    cq.Workplane("XY")
    .box(SLOT_LEN, 30, SLOT_T)
    .translate((u_end + SLOT_LEN / 2.0, 0, 0))
    .rotate((0, 0, 0), (0, 1, 0), SLOT_ANGLE)   # +X tips down toward -Z
    .translate((0, 0, z_slot))
)
body = body.cut(slot)

result = body
